import cadquery as cq

# camera for the harness render (default three-quarter view)
VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
L = 120.0          # plate length (X)
W = 60.0           # plate width (Y)
T_TOP = 1.5        # top (bezel) layer thickness
T_BOT = 1.5        # bottom (frame) layer thickness = pocket depth
R_CORNER = 7.5     # plan-view corner radius

# display window: 45 deg tapered opening through the top layer
WIN_L = 76.55      # window length at the bottom of the taper (X)
WIN_W = 38.8       # window width at the bottom of the taper (Y)
WIN_CX = -4.475    # window centre X (window sits toward -X)
WIN_CY = 0.1       # window centre Y

# pocket cut through the bottom layer (module recess with two end tabs)
PK_Y = 22.2        # half width of the pocket
PK_XN = -45.5      # pocket edge at the -X end
PK_XP = 44.5       # pocket edge at the +X end
TAB_N_X = -54.3    # -X tab reach
TAB_N_Y0, TAB_N_Y1 = -8.6, 8.7
TAB_P_X = 53.3     # +X tab reach
TAB_P_Y0, TAB_P_Y1 = -12.35, 11.4

# standoff bosses under the plate
BOSS_XN, BOSS_XP = -50.1, 49.4
BOSS_YN, BOSS_YP = -17.97, 18.55
BOSS_D = 4.4
BOSS_H = 4.5
RING_D = 7.4       # counterbore around each boss root
RING_DEPTH = 0.6   # counterbore depth

T = T_TOP + T_BOT

# ---------------- plate ----------------
plate = (
    cq.Workplane("XY")
    .sketch()
    .rect(L, W)
    .vertices()
    .fillet(R_CORNER)
    .finalize()
    .extrude(T)
)

# module pocket in the underside
pocket_pts = [
    (PK_XN, -PK_Y),
    (PK_XP, -PK_Y),
    (PK_XP, TAB_P_Y0),
    (TAB_P_X, TAB_P_Y0),
    (TAB_P_X, TAB_P_Y1),
    (PK_XP, TAB_P_Y1),
    (PK_XP, PK_Y),
    (PK_XN, PK_Y),
    (PK_XN, TAB_N_Y1),
    (TAB_N_X, TAB_N_Y1),
    (TAB_N_X, TAB_N_Y0),
    (PK_XN, TAB_N_Y0),
]
pocket = cq.Workplane("XY").polyline(pocket_pts).close().extrude(T_BOT)
plate = plate.cut(pocket)

# tapered window: a prism whose lower edges are chamfered at 45 deg
EXT = 1.0  # cutter overshoot below the pocket ceiling / above the top face
cut_h = T_TOP + 2 * EXT
cutter = (
    cq.Workplane("XY")
    .workplane(offset=T_BOT - EXT)
    .center(WIN_CX, WIN_CY)
    .rect(WIN_L + 2 * T_TOP, WIN_W + 2 * T_TOP)
    .extrude(cut_h)
    .faces("<Z")
    .edges()
    .chamfer(T_TOP + EXT)
)
plate = plate.cut(cutter)

# ---------------- standoff bosses (each rising from a shallow counterbore) ----------------
pts = [(x, y) for x in (BOSS_XN, BOSS_XP) for y in (BOSS_YN, BOSS_YP)]
rings = cq.Workplane("XY").pushPoints(pts).circle(RING_D / 2).extrude(RING_DEPTH)
plate = plate.cut(rings)
bosses = (
    cq.Workplane("XY")
    .workplane(offset=RING_DEPTH)
    .pushPoints(pts)
    .circle(BOSS_D / 2)
    .extrude(-(BOSS_H + RING_DEPTH))
)

result = plate.union(bosses)
